import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
T_TOP = 15.3          # top surface height (legs stand on Z=0)
ARM_T = 6.0           # arm plate thickness
CEIL_Z = 9.3          # underside of the box plate near the front
POCKET_Z = 8.3        # top of the pocket open to +X

# arm (L-shaped clamp plate)
STRIP_W = 10.3        # width of the long left strip
ARM_R_X = 36.3        # right end of the arm cross bar
ARM_R_Y0 = 20.0       # lower edge of the arm cross bar
ARM_Y1 = 31.4         # back edge of the arm (seam line)
ARM_CORNER_R = 4.7    # rounded outer corner of the arm
SLOT_CX, SLOT_CY, SLOT_R = 18.0, 18.0, 8.4   # U-slot for the hotend

# box under the lettered plate
BX0, BX1 = 4.7, 42.1  # box X extent
BY0, BY1 = 32.6, 60.3 # box Y extent
SEAM_Y1 = 34.1        # second seam line on the top face
FRONT_WALL = 3.4
BACK_WALL = 3.3
FL_X1 = 15.5          # front-left leg inner face
FR_X0 = 36.2          # right legs inner face
CH_X1 = 31.0          # right side of the flat-roofed front channel
BEVEL_X, BEVEL_Y = 2.0, 0.2    # bevel on the front-left leg's outer edge
ARCH_CX, ARCH_R, ARCH_ZC = 26.3, 11.5, -1.4   # tunnel along Y
BACK_CX, BACK_R = 26.0, 9.0                   # arch through the back wall
XT_R, XT_CY, XT_ZC = 11.1, 46.3, -0.5         # tunnel along X
XT_FLARE = 3.0        # 45 deg flare of the X tunnel at the -X face
TOP_EDGE_R = 1.25     # rounding of the +X top edge
CORNER_R = 1.4        # rounding of the vertical +X corners
BEAM_R = 0.9          # rounding of the beam over the +X pocket
LEG_IN_R = 1.8        # rounding of the legs' inner vertical +X corners

HOLE_S = 2.4          # small screw holes
HOLE_L = 4.3          # big holes in the plate
CBORE_D, CBORE_H = 4.2, 2.5
HEX_AF = 4.2
HEX_DEPTH = 2.6
ENGRAVE = 0.8
FONT = "DejaVu Sans"
CAP_H = 3.9           # lettering cap height

arm_z0 = T_TOP - ARM_T


def cyl_y(cx, cz, r, y0, y1):
    return cq.Workplane("XZ").center(cx, cz).circle(r).extrude(-(y1 - y0)).translate((0, y0, 0))


def cyl_x(cy, cz, r, x0, x1):
    return cq.Workplane("YZ").center(cy, cz).circle(r).extrude(x1 - x0).translate((x0, 0, 0))


def blk(x0, x1, y0, y1, z0, z1):
    return cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0, centered=False).translate((x0, y0, z0))


def vhole(x, y, d, z0=-10, z1=40):
    return cq.Workplane("XY").circle(d / 2).extrude(z1 - z0).translate((x, y, z0))


# ---------------- arm ----------------
arm = (
    cq.Workplane("XY")
    .moveTo(0, 0)
    .lineTo(STRIP_W, 0)
    .lineTo(STRIP_W, ARM_R_Y0)
    .lineTo(ARM_R_X, ARM_R_Y0)
    .lineTo(ARM_R_X, SEAM_Y1)
    .lineTo(BX0, SEAM_Y1)
    .lineTo(BX0, ARM_Y1)
    .threePointArc((BX0 - ARM_CORNER_R * math.sqrt(0.5), ARM_Y1 - ARM_CORNER_R * (1 - math.sqrt(0.5))),
                   (BX0 - ARM_CORNER_R, ARM_Y1 - ARM_CORNER_R))
    .close()
    .extrude(ARM_T)
    .translate((0, 0, arm_z0))
)
arm = arm.cut(
    cq.Workplane("XY").circle(SLOT_R).extrude(30).translate((SLOT_CX, SLOT_CY, -5))
    .union(blk(STRIP_W, 60, -10, SLOT_CY, -5, 25))
)

# ---------------- box envelope with rounded +X side ----------------
box = blk(BX0, BX1, BY0, BY1, 0, T_TOP)
box = box.edges("|Z and >X").fillet(CORNER_R)
# (the top fillet runs on along the tangent chain: +X, front and back top edges)
box = box.faces(">Z").edges(">X").fillet(TOP_EDGE_R)

# pocket open to +X, with a rounded beam edge over it
box = box.cut(blk(FR_X0, BX1 + 1, BY0 + FRONT_WALL, BY1 - BACK_WALL, -1, POCKET_Z))
for yy in (BY0 + FRONT_WALL, BY1 - BACK_WALL):   # round the legs' inner +X corners
    box = box.edges(cq.selectors.NearestToPointSelector((BX1, yy, POCKET_Z / 2))).fillet(LEG_IN_R)
box = box.edges(cq.selectors.NearestToPointSelector((BX1, (BY0 + BY1) / 2, POCKET_Z))).fillet(BEAM_R)

# front opening between the front legs (top corner on the right chamfered down
# to the pocket height), and a flat-roofed channel behind it on the left
front_open = (
    cq.Workplane("XZ")
    .polyline([(FL_X1, -1), (FL_X1, CEIL_Z), (CH_X1, CEIL_Z), (CH_X1 + 1.8, POCKET_Z),
               (FR_X0, POCKET_Z), (FR_X0, -1)]).close()
    .extrude(-(FRONT_WALL + 1.0))
    .translate((0, BY0 - 1.0, 0))
)
box = box.cut(front_open)
box = box.cut(blk(FL_X1, CH_X1, BY0, XT_CY, -1, CEIL_Z))
# tunnel along Y behind the front legs
box = box.cut(cyl_y(ARCH_CX, ARCH_ZC, ARCH_R, BY0 + FRONT_WALL, BY1 - BACK_WALL))
# arch through the back wall
box = box.cut(cyl_y(BACK_CX, 0, BACK_R, BY1 - BACK_WALL - 1, BY1 + 1))
# tunnel along X through the -X side, flared (45 deg) where it leaves the -X face
box = box.cut(cyl_x(XT_CY, XT_ZC, XT_R, BX0 - 1, FR_X0))
flare = cq.Solid.makeCone(XT_R + XT_FLARE + 1.0, XT_R, XT_FLARE + 1.0,
                          cq.Vector(BX0 - 1.0, XT_CY, XT_ZC), cq.Vector(1, 0, 0))
box = box.cut(cq.Workplane("XY").add(flare))
# shallow bevel on the outer front edge of the front-left leg
bevel = (
    cq.Workplane("XY")
    .polyline([(BX0 - 0.5, BY0 - 0.5), (BX0 + BEVEL_X, BY0 - 0.5), (BX0 + BEVEL_X, BY0),
               (BX0, BY0 + BEVEL_Y), (BX0 - 0.5, BY0 + BEVEL_Y)]).close()
    .extrude(CEIL_Z + 1.0)
    .translate((0, 0, -1.0))
)
box = box.cut(bevel)

part = box.union(arm)
# shallow seam strip between arm and lettered plate
part = part.cut(blk(BX0, ARM_R_X, ARM_Y1, SEAM_Y1, T_TOP - 0.06, T_TOP + 1))

# ---------------- holes ----------------
for (x, y) in [(7.5, 28.6), (29.1, 28.6), (7.5, 7.0)]:
    part = part.cut(vhole(x, y, HOLE_S))
    part = part.cut(vhole(x, y, CBORE_D, arm_z0 - 1, arm_z0 + CBORE_H))
for (x, y) in [(15.9, 56.4), (36.2, 56.4)]:
    part = part.cut(vhole(x, y, HOLE_S - 0.1, T_TOP - 6, T_TOP + 1))
for (x, y) in [(18.25, 38.4), (34.0, 38.4)]:
    part = part.cut(vhole(x, y, HOLE_L))
# hex nut traps from the top, small holes from below
hexw = cq.Workplane("XY").polygon(6, HEX_AF / math.cos(math.pi / 6)).extrude(HEX_DEPTH + 1)
part = part.cut(hexw.rotate((0, 0, 0), (0, 0, 1), 30).translate((5.65, 16.1, T_TOP - HEX_DEPTH)))
part = part.cut(hexw.translate((32.2, 22.8, T_TOP - HEX_DEPTH)))
for (x, y) in [(5.65, 16.1), (32.2, 22.8)]:
    part = part.cut(vhole(x, y, HOLE_S, arm_z0 - 1, T_TOP - HEX_DEPTH - 0.3))
# horizontal holes in the -X side of the plate
for y in [35.1, 57.8]:
    part = part.cut(cq.Workplane("YZ").center(y, 11.0).circle(1.0).extrude(6).translate((BX0 - 1, 0, 0)))
# small slot through the back-right corner, hole in the back-right foot
part = part.cut(blk(BX1 - 2.5, BX1 + 1, 56.3, BY1 + 1, 10.0, 11.7))
part = part.cut(vhole(39.2, 58.6, 1.8, -1, 5))

# ---------------- engraved lettering (reads along -X) ----------------
# (letter, centre X, ink width) for each line; the lettering is a wide block face,
# so every glyph is stretched to its measured width and scaled to the cap height.
LINE1 = [("A", 37.1, 4.7), ("R", 32.14, 3.7), ("G", 27.7, 4.1), ("E", 23.29, 3.3),
         ("N", 18.87, 3.7), ("T", 14.24, 3.7), ("O", 9.5, 4.3)]
LINE2 = [("H", 35.3, 5.3), ("o", 29.93, 3.55), ("t", 26.2, 2.55), ("e", 22.25, 3.95),
         ("n", 17.28, 4.15), ("d", 11.6, 4.95)]
BASE1, BASE2 = 44.45, 51.1


def glyph(ch, size):
    return cq.Workplane("XY").text(ch, size, ENGRAVE + 0.5, combine=False, halign="center",
                                   valign="bottom", font=FONT, kind="bold").val()


def letters(spec, y_base):
    ref = glyph("H", 10.0).BoundingBox()
    size = 10.0 * CAP_H / ref.ylen          # font size giving the wanted cap height
    solids = None
    for ch, xc, w in spec:
        g = glyph(ch, size)
        bb = g.BoundingBox()
        sx = w / bb.xlen
        g = g.transformGeometry(cq.Matrix([[sx, 0, 0, -sx * bb.center.x], [0, 1, 0, 0],
                                           [0, 0, 1, 0], [0, 0, 0, 1]]))
        g = g.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), 180)
        g = g.translate(cq.Vector(xc, y_base, T_TOP - ENGRAVE))
        solids = g if solids is None else solids.fuse(g)
    return solids


try:
    engraved = part.cut(letters(LINE1, BASE1)).cut(letters(LINE2, BASE2))
    if engraved.val().isValid():
        part = engraved
except Exception:
    pass   # lettering is cosmetic; keep the plain plate if the font is unavailable

result = part
